import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
X_LEN = 2120.0      # depth of the U along X (arm tips to back of the spine)
Y_LEN = 2700.0      # width of the U along Y
ARM_W = 706.0       # width of each arm (along Y) and of the spine (along X)
TABLE_H = 745.0     # overall height
TOP_T = 46.0        # top slab thickness
TOP_EDGE_R = 14.0   # rounding of the slab top edges
TOP_CORNER_R = 12.0 # rounding of the slab convex vertical corners
TOP_INNER_R = 8.0   # rounding of the two concave corners of the U
INSET = 57.0        # slab edge to outer face of legs / frame rails
LEG = 90.0          # square leg section
RAIL_H = 58.0       # frame rail height under the slab
RAIL_W = 90.0       # frame rail width (flush with the legs)
FOOT_L = 140.0      # foot plate length (along X)
FOOT_W = 100.0      # foot plate width (along Y)
FOOT_T = 12.0       # foot plate thickness
FOOT_R = 5.0        # foot plate corner radius (plan)
FOOT_EDGE_R = 3.0   # rounding of the foot plate bottom edges

Z_SLAB_BOT = TABLE_H - TOP_T
Z_RAIL_BOT = Z_SLAB_BOT - RAIL_H

# U outline (opening towards -X)
U_PTS = [
    (0.0, 0.0), (X_LEN, 0.0), (X_LEN, Y_LEN), (0.0, Y_LEN),
    (0.0, Y_LEN - ARM_W), (X_LEN - ARM_W, Y_LEN - ARM_W),
    (X_LEN - ARM_W, ARM_W), (0.0, ARM_W),
]
CONVEX = [U_PTS[i] for i in (0, 1, 2, 3, 4, 7)]
CONCAVE = [U_PTS[i] for i in (5, 6)]


def u_wire(offset=0.0):
    w = cq.Workplane("XY").polyline(U_PTS).close().wires().val()
    if offset:
        w = w.offset2D(-offset, "intersection")[0]
    return w


def near(pts, tol=1.0):
    sel = None
    for (px, py) in pts:
        s = cq.selectors.BoxSelector((px - tol, py - tol, -1e4), (px + tol, py + tol, 1e4))
        sel = s if sel is None else sel + s
    return sel


# ---------------- top slab ----------------
top = (
    cq.Workplane("XY").workplane(offset=Z_SLAB_BOT)
    .polyline(U_PTS).close().extrude(TOP_T)
)
top = top.edges("|Z").edges(near(CONVEX)).fillet(TOP_CORNER_R)
top = top.edges("|Z").edges(near(CONCAVE)).fillet(TOP_INNER_R)
top = top.faces(">Z").edges().fillet(TOP_EDGE_R)

# ---------------- frame rails under the slab ----------------
outer = u_wire(INSET)
inner = u_wire(INSET + RAIL_W)
frame = (
    cq.Workplane("XY").add(outer).toPending().extrude(RAIL_H)
    .cut(cq.Workplane("XY").add(inner).toPending().extrude(RAIL_H))
    .translate((0, 0, Z_RAIL_BOT))
)

# ---------------- legs ----------------
c0 = INSET + LEG / 2.0
xi = X_LEN - ARM_W + c0          # inner-corner legs, X position
LEG_XY = [
    (c0, c0), (c0, ARM_W - c0),                       # front arm tip
    (c0, Y_LEN - ARM_W + c0), (c0, Y_LEN - c0),       # back arm tip
    (X_LEN - c0, c0), (X_LEN - c0, Y_LEN - c0),       # spine outer corners
    (xi, ARM_W - c0), (xi, Y_LEN - ARM_W + c0),       # inner corners
]

legs = (
    cq.Workplane("XY").workplane(offset=FOOT_T)
    .pushPoints(LEG_XY).rect(LEG, LEG).extrude(Z_SLAB_BOT - FOOT_T)
)
feet = (
    cq.Workplane("XY").pushPoints(LEG_XY)
    .rect(FOOT_L, FOOT_W).extrude(FOOT_T)
    .edges("|Z").fillet(FOOT_R)
    .faces("<Z").edges().fillet(FOOT_EDGE_R)
)

body = top.union(frame).union(legs).union(feet)

# ---------------- mitered top panels ----------------
# The top is three panels meeting on 45 deg miters at the two outer corners;
# the miter joints are imprinted as seams on the flat top face.


def miter_plane(p0, p1):
    (x0, y0), (x1, y1) = p0, p1
    z0, z1 = Z_SLAB_BOT - 10.0, TABLE_H + 10.0
    pts = [cq.Vector(x0, y0, z0), cq.Vector(x1, y1, z0),
           cq.Vector(x1, y1, z1), cq.Vector(x0, y0, z1)]
    return cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True))


def on_front_miter(p):
    return abs(p.x + p.y - X_LEN) < 1e-3


def on_back_miter(p):
    return abs(p.x - p.y - (X_LEN - Y_LEN)) < 1e-3


M = 100.0
xi_c = X_LEN - ARM_W
miters = [
    (miter_plane((X_LEN + M, -M), (xi_c - M, ARM_W + M)), on_front_miter),
    (miter_plane((X_LEN + M, Y_LEN + M), (xi_c - M, Y_LEN - ARM_W - M)), on_back_miter),
]
# split the flat top face with the miter planes and keep the new seam edges
top_face = body.faces(">Z").val()
top_pieces = top_face.split(*[plane for plane, _ in miters])
seams = []
for e in top_pieces.Edges():
    a, b = e.startPoint(), e.endPoint()
    if any(on(a) and on(b) for _, on in miters):
        seams.append(e)
# imprint the seams on the body (one solid, top face split into three panels)
result = cq.Workplane("XY").add(body.val().split(*seams))
result = result.translate((-X_LEN / 2.0, -Y_LEN / 2.0, 0))

VIEW = {"azimuth": 45, "elevation": 26}
